import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 40            # number of teeth
MODULE = 2.0            # gear module
PRESSURE_ANGLE = 20.0   # degrees
ADDENDUM = 1.0 * MODULE
DEDENDUM = 1.25 * MODULE
FACE_WIDTH = 4.5        # gear thickness along X (gear axis = X)
BORE_L = 4.0            # obround bore length (along Y)
BORE_W = 3.0            # obround bore width  (along Z)
TOOTH_PHASE = 90.0      # angular position of a tooth centre (deg, 90 = +Z)
FLANK_PTS = 5           # involute sample points per flank
ROOT_PTS = 4            # interior sample points on the root fillet

# ---------------- derived gear geometry ----------------
r_p = MODULE * N_TEETH / 2.0                       # pitch radius
r_b = r_p * math.cos(math.radians(PRESSURE_ANGLE))  # base radius
r_a = r_p + ADDENDUM                               # tip radius
r_f = r_p - DEDENDUM                               # root radius
alpha = math.radians(PRESSURE_ANGLE)
inv_a = math.tan(alpha) - alpha
beta0 = math.pi / (2 * N_TEETH) + inv_a            # half tooth angle at base
half_pitch = math.pi / N_TEETH
pitch = 2.0 * half_pitch


def t_of_r(r):
    """Involute roll parameter for radius r."""
    return math.sqrt(max((r / r_b) ** 2 - 1.0, 0.0))


def left_flank(t):
    """Point / outward unit tangent on the left flank of a tooth centred on angle 0."""
    x = r_b * (math.cos(t) + t * math.sin(t))
    y = -r_b * (math.sin(t) - t * math.cos(t))
    c, s = math.cos(beta0), math.sin(beta0)
    p = (c * x - s * y, s * x + c * y)
    d = (math.cos(beta0 - t), math.sin(beta0 - t))
    return p, d


def root_circle(r_s):
    """Fillet circle tangent to both flanks of a tooth space at radius r_s.
    Returns (start point, centre, radius, bottom radius)."""
    p, d = left_flank(t_of_r(r_s))
    n = (-d[1], d[0])
    u = (math.cos(half_pitch), math.sin(half_pitch))
    v = (-u[1], u[0])
    R = -(p[0] * v[0] + p[1] * v[1]) / (n[0] * v[0] + n[1] * v[1])
    c = (p[0] + R * n[0], p[1] + R * n[1])
    return p, c, R, c[0] * u[0] + c[1] * u[1] - R


# flank start radius at which the tangent root fillet just reaches r_f
lo, hi = max(r_b, r_f) + 1e-6, r_a - 1e-3
for _ in range(80):
    mid = 0.5 * (lo + hi)
    if root_circle(mid)[3] > r_f:
        hi = mid
    else:
        lo = mid
r_s = 0.5 * (lo + hi)


def rot(p, a):
    c, s = math.cos(a), math.sin(a)
    return (c * p[0] - s * p[1], s * p[0] + c * p[1])


def mirror_about(p, a):
    """Mirror point/vector p about the line through the origin at angle a."""
    c, s = math.cos(2 * a), math.sin(2 * a)
    return (c * p[0] + s * p[1], s * p[0] - c * p[1])


# ---- one tooth space (between tooth at angle 0 and tooth at angle pitch) ----
t_s, t_a = t_of_r(r_s), t_of_r(r_a)
# involute samples evenly spaced in arc length (arc length ~ t^2)
flank_t = [math.sqrt(t_a ** 2 - (t_a ** 2 - t_s ** 2) * i / (FLANK_PTS - 1))
           for i in range(FLANK_PTS)]                       # tip -> r_s
down_flank = [left_flank(t)[0] for t in flank_t]
down_tan = [(-left_flank(t)[1][0], -left_flank(t)[1][1]) for t in flank_t]

p_s, c_root, R_root, _ = root_circle(r_s)
a0 = math.atan2(p_s[1] - c_root[1], p_s[0] - c_root[0])
a_bottom = half_pitch + math.pi                             # lowest point of fillet
half_sweep = math.atan2(math.sin(a_bottom - a0), math.cos(a_bottom - a0))
sweep = 2.0 * half_sweep                                    # signed, via the bottom
sgn = 1.0 if sweep > 0 else -1.0
root_pts, root_tan = [], []
for i in range(1, ROOT_PTS + 1):
    ang = a0 + sweep * i / (ROOT_PTS + 1)
    root_pts.append((c_root[0] + R_root * math.cos(ang),
                     c_root[1] + R_root * math.sin(ang)))
    root_tan.append((-sgn * math.sin(ang), sgn * math.cos(ang)))

up_flank = [mirror_about(p, half_pitch) for p in reversed(down_flank)]
up_tan = [mirror_about((-d[0], -d[1]), half_pitch) for d in reversed(down_tan)]

# tooth space curve (tip of tooth k -> tip of tooth k+1) with exact tangents
gap_pts = down_flank + root_pts + up_flank
gap_tan = down_tan + root_tan + up_tan

# ---------------- gear outline (local x = global Y, local y = global Z) -----
start_angle = math.radians(TOOTH_PHASE)   # one tooth points straight up (+Z)
first = rot(mirror_about(down_flank[0], 0.0), start_angle)  # right tip corner

wp = cq.Workplane("YZ").workplane(offset=-FACE_WIDTH / 2.0).moveTo(*first)
for k in range(N_TEETH):
    a = start_angle + k * pitch
    # tip land (arc on the tip circle)
    wp = wp.threePointArc((r_a * math.cos(a), r_a * math.sin(a)),
                          rot(down_flank[0], a))
    # tooth space: flank - root fillet - flank as one smooth curve
    pts = [rot(p, a) for p in gap_pts]
    if k == N_TEETH - 1:
        pts[-1] = first
    wp = wp.spline(pts[1:], tangents=[rot(d, a) for d in gap_tan],
                   includeCurrent=True)
wp = wp.close()
gear = wp.extrude(FACE_WIDTH)

# ---------------- obround bore ----------------
bore = (
    cq.Workplane("YZ")
    .workplane(offset=-FACE_WIDTH)
    .slot2D(BORE_L, BORE_W, 0)
    .extrude(2 * FACE_WIDTH)
)
result = gear.cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
